import cadquery as cq
import math

# ---------------- driving dimensions (mm) ----------------
R_FLANGE = 50.0      # flange outer radius
T_FLANGE = 7.1       # flange thickness
RIM_A = 6.7          # rim rounding, horizontal semi-axis (elliptic full round)
RIM_B = 7.1          # rim rounding, vertical semi-axis (= flange thickness)

H_THREAD = 14.55     # height of threaded spigot below the flange
PITCH = 4.7          # thread pitch (right hand, round profile)
R_CREST = 41.4       # thread crest radius
R_ROOT = 39.4        # thread root radius (spigot core)
THREAD_PHASE = 4.12  # height of a crest on the +X side (mod pitch)
ROOT_GAP = 0.1       # half width of the root land between thread turns
EMBED = 0.6          # how far the swept ridge reaches into the core

R_HOLE = 28.6        # top bore radius (through the flange top)
D_HOLE = 3.7         # depth of the top bore below the top face
R_MID = 32.3         # bore radius just under the internal shoulder
F_SHOULDER = 1.2     # fillet in the shoulder / bore corner
Z_MID = 14.35        # height where the drafted spigot bore starts
R_BOT = 34.2         # bore radius at the bottom face (drafted bore)

SEAM_OUT = 135.0     # angular position of the revolve seam of the outer skin
SEAM_IN = 225.0      # angular position of the revolve seam of the bore

H_TOTAL = H_THREAD + T_FLANGE
Z_SHOULDER = H_TOTAL - D_HOLE

# ---------------- flange + spigot core (revolved) ----------------
prof = (
    cq.Workplane("XZ")
    .moveTo(0, 0)
    .lineTo(R_ROOT, 0)
    .lineTo(R_ROOT, H_THREAD)
    .lineTo(R_FLANGE, H_THREAD)
    # elliptic full round on the flange rim, tangent to the flat top face
    .ellipseArc(RIM_A, RIM_B, angle1=0, angle2=90, startAtCurrent=True)
    .lineTo(0, H_TOTAL)
    .close()
)
body = prof.revolve(360, (0, 0, 0), (0, 1, 0)).rotate((0, 0, 0), (0, 0, 1), SEAM_OUT)

# ---------------- helical thread ridge (round crest) ----------------
sag = R_CREST - R_ROOT
rho = (sag ** 2 + (PITCH / 2.0) ** 2) / (2.0 * sag)   # crest arc radius
rc = R_CREST - rho                                     # crest arc centre radius
hw = PITCH / 2.0 - ROOT_GAP                            # half width of the ridge
r_hw = rc + math.sqrt(rho ** 2 - hw ** 2)              # arc radius at +-hw

z_start = THREAD_PHASE - 2.0 * PITCH                   # start well below z = 0
turns = math.ceil((H_THREAD + PITCH - z_start) / PITCH)
helix = cq.Wire.makeHelix(PITCH, turns * PITCH, R_ROOT)

ridge_prof = (
    cq.Workplane("XZ")
    .moveTo(R_ROOT - EMBED, -hw)
    .lineTo(r_hw, -hw)
    .threePointArc((R_CREST, 0), (r_hw, hw))
    .lineTo(R_ROOT - EMBED, hw)
    .close()
)
ridge = ridge_prof.sweep(cq.Workplane().add(helix), isFrenet=True)
ridge = ridge.translate((0, 0, z_start))

# keep only the part of the ridge between the bottom face and the flange
clip = (
    cq.Workplane("XY")
    .circle(R_CREST + 2.0)
    .circle(R_ROOT - 2.0 * EMBED)
    .extrude(H_THREAD)
)
ridge = ridge.intersect(clip)

body = body.union(ridge)

# ---------------- bore (void) profile ----------------
eps = 1.0
draft = (R_BOT - R_MID) / Z_MID                      # radial growth per mm down
f = F_SHOULDER
fc = (R_MID - f, Z_SHOULDER - f)                     # fillet centre
bore = (
    cq.Workplane("XZ")
    .moveTo(0, -eps)
    .lineTo(R_BOT + draft * eps, -eps)
    .lineTo(R_MID, Z_MID)                            # drafted spigot bore
    .lineTo(R_MID, Z_SHOULDER - f)
    .threePointArc((fc[0] + f * math.cos(math.pi / 4), fc[1] + f * math.sin(math.pi / 4)),
                   (R_MID - f, Z_SHOULDER))          # rounded shoulder corner
    .lineTo(R_HOLE, Z_SHOULDER)                      # internal shoulder
    .lineTo(R_HOLE, H_TOTAL + eps)                   # top bore
    .lineTo(0, H_TOTAL + eps)
    .close()
    .revolve(360, (0, 0, 0), (0, 1, 0))
    .rotate((0, 0, 0), (0, 0, 1), SEAM_IN)
)

result = body.cut(bore)

VIEW = {"azimuth": 45, "elevation": 26}
